import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_X = 85.0          # width along X
PLATE_Y = 100.0         # length along Y
BODY_T = 6.2            # main plate thickness (above the lip)
CORNER_R = 8.0          # plan-view corner radius
TOP_FILLET = 2.3        # rounded top edge
BOT_FILLET = 0.4        # small bottom edge round

LIP_INSET = 2.0         # locating lip inset from outer edge
LIP_H = 0.5             # lip protrusion below the body
LIP_T = 0.4             # lip wall thickness
CAVITY_D = 3.0          # underside cavity depth (measured from lip bottom)

GRILLE_CX = 13.5        # grille centre (from plate centre)
GRILLE_CY = -13.5
GRILLE_D = 32.8         # grille circle diameter
BAR_COUNT = 7           # bars left across the grille opening
BAR_PITCH = 4.3
BAR_W = 2.2


def rrect(w, h, r, z0, height):
    return (
        cq.Workplane("XY", origin=(0, 0, z0))
        .sketch()
        .rect(w, h)
        .vertices()
        .fillet(r)
        .finalize()
        .extrude(height)
    )


# ---------------- main plate ----------------
body = rrect(PLATE_X, PLATE_Y, CORNER_R, 0.0, BODY_T)
body = body.faces(">Z").edges().fillet(TOP_FILLET)
body = body.faces("<Z").edges().fillet(BOT_FILLET)

# locating lip / pad below the plate
pad = rrect(PLATE_X - 2 * LIP_INSET, PLATE_Y - 2 * LIP_INSET,
            CORNER_R - LIP_INSET, -LIP_H, LIP_H)
body = body.union(pad)

# underside cavity inside the lip
ci = LIP_INSET + LIP_T
cavity = rrect(PLATE_X - 2 * ci, PLATE_Y - 2 * ci, CORNER_R - ci,
               -LIP_H - 1.0, CAVITY_D + 1.0)
body = body.cut(cavity)

# ---------------- grille: circular opening with bars left across it ----------------
z0 = -LIP_H - 1.0
h = BODY_T + LIP_H + 2.0
hole = (
    cq.Workplane("XY", origin=(GRILLE_CX, GRILLE_CY, z0))
    .circle(GRILLE_D / 2.0)
    .extrude(h)
)
bars = None
for i in range(BAR_COUNT):
    x = GRILLE_CX + (i - (BAR_COUNT - 1) / 2.0) * BAR_PITCH
    b = (
        cq.Workplane("XY", origin=(x, GRILLE_CY, z0))
        .rect(BAR_W, GRILLE_D + 2.0)
        .extrude(h)
    )
    bars = b if bars is None else bars.union(b)
cutter = hole.cut(bars)
result = body.cut(cutter)

VIEW = {"azimuth": 45, "elevation": 26}
